import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------------------------------------------------------------------
# Oblique slice of a round bar carrying a hex-ended recess (cap-nut section).
# Built in a local "plate" frame: x = long axis of the cut face, z = up,
# y = into the part (front face at y = -WF).  Finally rotated 45 deg about Z
# so the bar axis ends up along world Y.
# ---------------------------------------------------------------------------
R = 20.0                 # radius of the round bar (axis along world Y)
WF = 0.22 * R            # front cut plane offset from the bar axis
WB0 = -0.185 * R         # back cut plane offset (at local x = 0)
KB = -0.020              # slight twist of the back cut plane (dw/du)
D = 0.215 * R            # pocket depth
RF = 0.97 * D            # (nearly full-round) fillet at the pocket floor
ROT = 45.0               # angle of the cut planes about Z

# outer hex-like end (front-face profile, local x,z)
UL = -1.267 * R          # end flat position
ZL = 0.32 * R            # half height of the end flat
U1, Z1 = -0.882 * R, 0.775 * R   # corner between flat 1 and flat 2
U2, Z2 = -0.408 * R, 1.14 * R     # flat 2 continues out past the bar

# spherical turning of the hex end (local frame: centre x, plate-normal offset)
UC, WS, RS = -0.39 * R, 0.317 * R, 0.9987 * R
WNB = -0.155 * R         # the spherical turning stops short of the back cut

# pocket profile
UP = -1.105 * R          # pocket end flat
ZP0 = 0.262 * R          # half height of pocket end flat
ZP = 0.808 * R           # pocket half height

# grooves (world frame)
XG = -0.172 * R          # V groove along world Y (top & bottom), at world x
YG = -0.075 * R          # V groove along world X (top & bottom), at world y
VGY = 0.055 * R          # depth of the Y groove
ZAX = 0.927 * R          # apex height of the X groove
VANG = 60.0              # included angle of the V grooves
SW, SD = 0.042 * R, 0.010 * R   # shallow slot along the bar on the world +X side
SY0 = 1.03 * R                  # world y where that slot starts

BIG = 4.0 * R

# ---- bar along world Y, expressed in the local frame (axis (1,1,0)/sqrt2)
axis = cq.Vector(1, 1, 0).normalized()
bar = cq.Solid.makeCylinder(R, 2 * BIG, cq.Vector(0, 0, 0) - axis * BIG, axis)

# ---- hex-like end profile extruded along the plate normal, behind the front
outer_pts = [
    (UL, -ZL), (UL, ZL), (U1, Z1), (U2, Z2), (BIG, Z2),
    (BIG, -Z2), (U2, -Z2), (U1, -Z1),
]
slab = (
    cq.Workplane("XZ", origin=(0, BIG, 0))
    .polyline(outer_pts).close()
    .extrude(BIG + WF)
)
body = slab.intersect(cq.Workplane().add(bar))

# ---- the hex end is turned spherical (dome of radius RS) rather than
#      cylindrical, so it stands slightly proud of the bar on the flats
dome = cq.Solid.makeSphere(RS, cq.Vector(UC, -WS, 0), angleDegrees1=-90, angleDegrees2=90)
nut = slab.intersect(cq.Workplane().add(dome))
nut = nut.cut(cq.Workplane("XY").box(4 * BIG, 2 * BIG, 4 * BIG).translate((0, BIG - WNB, 0)))
body = body.union(nut)

# ---- back cut plane (w = WB0 + KB*u  ->  y = -WB0 - KB*x)
back = (
    cq.Workplane("XY").box(4 * BIG, 2 * BIG, 4 * BIG)
    .translate((0, BIG, 0))
    .rotate((0, 0, 0), (0, 0, 1), -math.degrees(math.atan(KB)))
    .translate((0, -WB0, 0))
)
body = body.cut(back)

# ---- recess in the front face, rounded at the floor
pk_pts = [
    (UP, -ZP0), (UP, ZP0), (UP + (ZP - ZP0), ZP), (BIG, ZP),
    (BIG, -ZP), (UP + (ZP - ZP0), -ZP),
]
EXTRA = 2.0
pocket = (
    cq.Workplane("XZ", origin=(0, -WF + D, 0))
    .polyline(pk_pts).close()
    .extrude(D + EXTRA)
    .faces(">Y").edges()
    .fillet(RF)
)
body = body.cut(pocket)

# rotate into the world frame
body = body.rotate((0, 0, 0), (0, 0, 1), ROT)

# ---- grooves (world frame)
tn = math.tan(math.radians(VANG / 2.0))


def v_tool(plane, origin, c0, z_apex, sign, length):
    # triangular prism: apex at (c0, z_apex), opening away from the part
    h = 0.25 * R
    pts = [(c0 - h * tn, z_apex + sign * h), (c0 + h * tn, z_apex + sign * h), (c0, z_apex)]
    return cq.Workplane(plane, origin=origin).polyline(pts).close().extrude(length)


zt = math.sqrt(R * R - XG * XG)
for sgn in (1, -1):
    body = body.cut(v_tool("XZ", (0, BIG, 0), XG, sgn * (zt - VGY), sgn, 2 * BIG))
    body = body.cut(v_tool("YZ", (-BIG, 0, 0), YG, sgn * ZAX, sgn, 2 * BIG))

slot = (
    cq.Workplane("XY").box(2 * SD, 2 * BIG, SW)
    .translate((R, SY0 + BIG, 0))
)
body = body.cut(slot)

result = body
